import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 125.0          # overall length in X (wall outer face -> flange outer face)
W = 150.0          # overall width in Y
T = 4.7            # material thickness (plate, walls, tabs)

# top plate outline
CH_X0 = 78.2       # chamfer start (x) on the +/-Y edges
TAB_HW = 48.6      # half width of the +X tab
CH_X1 = 104.6      # chamfer end (x)
R_CORNER = 4.7     # vertical corner radius at the +X tab corners (<= T)

# plate notches from the +/-Y edges
NOTCH_X0, NOTCH_X1, NOTCH_D = 11.6, 19.75, 15.8
# rectangular slots (17.7 x 11.2)
SLOT_A = 17.7
SLOT_B = 11.2
SLOT_SIDE_X = 42.55    # centre x of the two slots near the +/-Y edges
SLOT_SIDE_Y = 61.5     # centre |y|
SLOT_MID_X = 13.45     # centre x of middle slot (rotated 90 deg)
# plate holes
HOLE_D = 5.5
PLATE_HOLES = [(72.0, 67.1), (72.0, -67.1), (12.7, 40.5), (12.7, -40.5), (114.1, 0.0)]

# -X wall
WALL_H_OUT = 39.7      # depth of the wall at its outer face
WALL_H_IN = 37.9       # depth at its inner face (bevelled bottom)
END_TAB_X = 11.6       # return tabs at both wall ends
END_TAB_H = 17.0
END_HOLE_D = 5.2
END_HOLE_X = 5.8
END_HOLE_Z = -11.2
WIN_Y0, WIN_Y1 = 62.7, 70.3          # windows next to the return tabs
WALL_NOTCH_Y0, WALL_NOTCH_Y1 = 46.7, 62.7
WALL_NOTCH_TOP = -21.8
T_BAR_HW, T_BAR_Z0, T_BAR_Z1 = 23.3, -7.2, -22.6
T_STEM_HW = 8.0
FLAP_T = 1.7            # the two tongues beside the T stem are thinned to this

# +X flange
FLANGE_H = 40.8
FL_NOTCH_Y0, FL_NOTCH_Y1 = 16.3, 41.4
FL_NOTCH_TOP = -25.2

# hanging bars under the plate
BAR_BOTTOM = -21.2
BAR_R = 6.0
BAR_HOLE_D = 4.8
BAR_CSK_D = 8.8
BAR_HOLE_Z = -15.2
BAR1_Y_OUT, BAR1_Y_IN = 51.7, 47.0     # X-direction bars at +/-Y
BAR1_X0, BAR1_X1 = 8.3, 77.6
BAR2_X0, BAR2_X1 = 23.3, 28.0          # Y-direction bar
BAR2_HW = 35.0


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


# ---------------- plate outline ----------------
c45 = math.cos(math.radians(45))


def outline():
    return (cq.Workplane("XY")
           .moveTo(0, -W / 2)
           .lineTo(CH_X0, -W / 2)
           .lineTo(CH_X1, -TAB_HW)
           .lineTo(L - R_CORNER, -TAB_HW)
           .threePointArc((L - R_CORNER + R_CORNER * c45, -TAB_HW + R_CORNER - R_CORNER * c45),
                          (L, -TAB_HW + R_CORNER))
           .lineTo(L, TAB_HW - R_CORNER)
           .threePointArc((L - R_CORNER + R_CORNER * c45, TAB_HW - R_CORNER + R_CORNER * c45),
                          (L - R_CORNER, TAB_HW))
           .lineTo(CH_X1, TAB_HW)
           .lineTo(CH_X0, W / 2)
           .lineTo(0, W / 2)
           .close())


plate = outline().extrude(-T)


# +X flange: the outer strip of the tab, wrapping round the rounded corners
def flange_outline():
    wp = cq.Workplane("XY").moveTo(L - T, -TAB_HW)
    if R_CORNER < T:
        wp = wp.lineTo(L - R_CORNER, -TAB_HW)
    wp = (wp.threePointArc((L - R_CORNER + R_CORNER * c45, -TAB_HW + R_CORNER - R_CORNER * c45),
                           (L, -TAB_HW + R_CORNER))
          .lineTo(L, TAB_HW - R_CORNER)
          .threePointArc((L - R_CORNER + R_CORNER * c45, TAB_HW - R_CORNER + R_CORNER * c45),
                         (L - R_CORNER, TAB_HW)))
    if R_CORNER < T:
        wp = wp.lineTo(L - T, TAB_HW)
    return wp.close()


flange = flange_outline().extrude(-FLANGE_H)
for s in (1, -1):
    y0, y1 = sorted((s * FL_NOTCH_Y0, s * FL_NOTCH_Y1))
    flange = flange.cut(box(L - T - 1, L + 1, y0, y1, -FLANGE_H - 1, FL_NOTCH_TOP))

# ---------------- -X wall (bevelled bottom) ----------------
wall = (cq.Workplane("XZ")
        .polyline([(0, 0), (T, 0), (T, -WALL_H_IN), (0, -WALL_H_OUT)]).close()
        .extrude(W / 2, both=True))
for s in (1, -1):
    # windows beside the return tabs
    y0, y1 = sorted((s * WIN_Y0, s * WIN_Y1))
    wall = wall.cut(box(-1, T + 1, y0, y1, -END_TAB_H, -T))
    # notches from the bottom
    y0, y1 = sorted((s * WALL_NOTCH_Y0, s * WALL_NOTCH_Y1))
    wall = wall.cut(box(-1, T + 1, y0, y1, -FLANGE_H - 2, WALL_NOTCH_TOP))
# T shaped cut-out
wall = wall.cut(box(-1, T + 1, -T_BAR_HW, T_BAR_HW, T_BAR_Z1, T_BAR_Z0))
wall = wall.cut(box(-1, T + 1, -T_STEM_HW, T_STEM_HW, -FLANGE_H - 2, T_BAR_Z1 + 0.01))
# thinned tongues below the T bar
for s in (1, -1):
    y0, y1 = sorted((s * T_STEM_HW, s * T_BAR_HW))
    wall = wall.cut(box(FLAP_T, T + 1, y0, y1, -FLANGE_H - 2, T_BAR_Z1 + 0.01))

# return tabs at both ends with pin holes
tabs = None
for s in (1, -1):
    y0, y1 = sorted((s * W / 2, s * (W / 2 - T)))
    tab = box(0, END_TAB_X, y0, y1, -END_TAB_H, 0)
    tabs = tab if tabs is None else tabs.union(tab)

# ---------------- hanging bars ----------------
def csk_cutter(p, d_in, length):
    """countersunk hole: cone (90 deg) at point p on a face, drilled along unit vector d_in"""
    v = cq.Vector(*d_in)
    base = cq.Vector(*p) - v * 0.5
    cone = cq.Solid.makeCone(BAR_CSK_D / 2 + 0.5, 0.0, BAR_CSK_D / 2 + 0.5, base, v)
    cyl = cq.Solid.makeCylinder(BAR_HOLE_D / 2, length + 1.0, base, v)
    return cq.Workplane("XY").add(cone.fuse(cyl))


bars = None
for s in (1, -1):
    y0, y1 = sorted((s * BAR1_Y_IN, s * BAR1_Y_OUT))
    b = box(BAR1_X0, BAR1_X1, y0, y1, BAR_BOTTOM, -T / 2)
    b = b.edges("|Y").edges("<Z").fillet(BAR_R)
    for hx in (BAR1_X0 + BAR_R, BAR1_X1 - BAR_R):
        # countersunk from the inner face of the bar
        b = b.cut(csk_cutter((hx, s * BAR1_Y_IN, BAR_HOLE_Z), (0, s, 0), BAR1_Y_OUT - BAR1_Y_IN))
    bars = b if bars is None else bars.union(b)

bar2 = box(BAR2_X0, BAR2_X1, -BAR2_HW, BAR2_HW, BAR_BOTTOM, -T / 2)
bar2 = bar2.edges("|X").edges("<Z").fillet(BAR_R)
for hy in (-BAR2_HW + BAR_R, BAR2_HW - BAR_R):
    # countersunk from the +X face
    bar2 = bar2.cut(csk_cutter((BAR2_X1, hy, BAR_HOLE_Z), (-1, 0, 0), BAR2_X1 - BAR2_X0))

# ---------------- assemble ----------------
body = plate.union(flange).union(wall).union(tabs).union(bars).union(bar2)

# pin holes through the return tabs (and the wall behind them)
for s in (1, -1):
    y0, y1 = sorted((s * (W / 2 - T - 0.01), s * (W / 2 + 1)))
    pin = (cq.Workplane("XZ").center(END_HOLE_X, END_HOLE_Z).circle(END_HOLE_D / 2)
           .extrude(W / 2 + 2, both=True)).intersect(box(-1, END_TAB_X + 1, y0, y1, -END_TAB_H - 1, 1))
    body = body.cut(pin)

# plate notches
for s in (1, -1):
    y0, y1 = sorted((s * W / 2 + s, s * (W / 2 - NOTCH_D)))
    body = body.cut(box(NOTCH_X0, NOTCH_X1, y0, y1, -T - 1, 1))

# slots
for s in (1, -1):
    body = body.cut(box(SLOT_SIDE_X - SLOT_A / 2, SLOT_SIDE_X + SLOT_A / 2,
                        s * SLOT_SIDE_Y - SLOT_B / 2, s * SLOT_SIDE_Y + SLOT_B / 2,
                        -T - 1, 1))
body = body.cut(box(SLOT_MID_X - SLOT_B / 2, SLOT_MID_X + SLOT_B / 2,
                    -SLOT_A / 2, SLOT_A / 2, -T - 1, 1))

# plate holes
holes = (cq.Workplane("XY").workplane(offset=1)
         .pushPoints(PLATE_HOLES).circle(HOLE_D / 2).extrude(-T - 2))
body = body.cut(holes)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
